import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
T = 27.7            # plate thickness (along X)
R = 30.0            # radius of the round hub at the bottom
HEAD_R = 11.9       # radius of the knob at the top
HEAD_Z = 76.85      # height of knob centre above hub centre
NECK_W45 = 10.15    # neck half width at Z = 45
NECK_TAPER = 0.083  # half-width growth per mm going down
SHOULDER_Y = R      # right face of the shoulder block (tangent to hub)
SHOULDER_RC = 11.0  # convex corner radius of the shoulder
SHOULDER_CZ = 23.6  # height of the shoulder corner-arc centre
F_HUB = 19.0        # concave fillet neck(left) -> hub
F_SHOULDER = 12.0   # concave fillet neck(right) -> shoulder corner arc
F_HEAD = 9.0        # concave fillet neck -> head
EDGE_R = 3.5        # round-over of both flat faces

D_R = 6.65          # D-bore radius (through X)
D_FLAT = 4.55       # distance from bore axis to the flat (flat below)
BOT_D = 14.0        # blind hole from the bottom (along Z)
BOT_DEPTH = 16.0


# ---------------- small 2D helpers (u = Y, v = Z) ----------------
def add(a, b):
    return (a[0] + b[0], a[1] + b[1])


def sub(a, b):
    return (a[0] - b[0], a[1] - b[1])


def mul(a, s):
    return (a[0] * s, a[1] * s)


def dot(a, b):
    return a[0] * b[0] + a[1] * b[1]


def norm(a):
    l = math.hypot(a[0], a[1])
    return (a[0] / l, a[1] / l)


def line_circle_fillet(p, d, n, c, rc, rf, pick_max):
    """Concave fillet between line (point p, dir d, outward normal n)
    and circle (centre c, radius rc). Returns (centre, tangent on line,
    tangent on circle)."""
    q = sub(add(p, mul(n, rf)), c)
    b = dot(q, d)
    cc = dot(q, q) - (rc + rf) ** 2
    disc = math.sqrt(b * b - cc)
    t = (-b + disc) if pick_max else (-b - disc)
    f = add(add(p, mul(n, rf)), mul(d, t))
    t_line = sub(f, mul(n, rf))
    t_circ = add(c, mul(norm(sub(f, c)), rc))
    return f, t_line, t_circ


def arc_mid(center, a, b, r):
    m = norm(add(sub(a, center), sub(b, center)))
    return add(center, mul(m, r))


# ---------------- neck lines ----------------
kn = math.sqrt(1.0 + NECK_TAPER ** 2)
# right neck line: Y = W45 + k (45 - Z)
pR = (NECK_W45, 45.0)
dR = (-NECK_TAPER / kn, 1.0 / kn)
nR = (1.0 / kn, NECK_TAPER / kn)
# left neck line (mirror)
pL = (-NECK_W45, 45.0)
dL = (NECK_TAPER / kn, 1.0 / kn)
nL = (-1.0 / kn, NECK_TAPER / kn)

hub_c = (0.0, 0.0)
head_c = (0.0, HEAD_Z)

# shoulder corner arc (convex)
cC = (SHOULDER_Y - SHOULDER_RC, SHOULDER_CZ)
A0 = (SHOULDER_Y, 0.0)
A1 = (SHOULDER_Y, SHOULDER_CZ)
# fillet neck-right / shoulder corner arc
fS, B2, B1 = line_circle_fillet(pR, dR, nR, cC, SHOULDER_RC, F_SHOULDER, True)

# fillet neck-right / head
fH_R, B3, B4 = line_circle_fillet(pR, dR, nR, head_c, HEAD_R, F_HEAD, False)
# fillet neck-left / head
fH_L, B6, B5 = line_circle_fillet(pL, dL, nL, head_c, HEAD_R, F_HEAD, False)
# fillet neck-left / hub
fB_L, B7, B8 = line_circle_fillet(pL, dL, nL, hub_c, R, F_HUB, True)


# hub arc from B8 (upper left) ccw round the bottom to A0
a8 = math.atan2(B8[1], B8[0])
a_end = 2.0 * math.pi
a_mid = 0.5 * (a8 + a_end)
hub_mid = (R * math.cos(a_mid), R * math.sin(a_mid))

prof = (
    cq.Workplane("YZ")
    .moveTo(*A0)
    .lineTo(*A1)
    .threePointArc(arc_mid(cC, A1, B1, SHOULDER_RC), B1)
    .threePointArc(arc_mid(fS, B1, B2, F_SHOULDER), B2)
    .lineTo(*B3)
    .threePointArc(arc_mid(fH_R, B3, B4, F_HEAD), B4)
    .threePointArc((0.0, HEAD_Z + HEAD_R), B5)
    .threePointArc(arc_mid(fH_L, B5, B6, F_HEAD), B6)
    .lineTo(*B7)
    .threePointArc(arc_mid(fB_L, B7, B8, F_HUB), B8)
    .threePointArc(hub_mid, A0)
    .close()
)

body = prof.extrude(T / 2.0, both=True)

# round-over of both flat faces
body = body.faces("<X or >X").edges().fillet(EDGE_R)

# D-shaped through bore along X
bore = cq.Workplane("YZ").workplane(offset=-T).circle(D_R).extrude(2 * T)
keep = (
    cq.Workplane("XY")
    .box(3 * T, 4 * D_R, 4 * D_R, centered=(True, True, False))
    .translate((0, 0, -D_FLAT))
)
dcut = bore.intersect(keep)
body = body.cut(dcut)

# blind hole from the bottom (set screw) along Z
bot = (
    cq.Workplane("XY")
    .workplane(offset=-R - 1.0)
    .circle(BOT_D / 2.0)
    .extrude(BOT_DEPTH + 1.0)
)
body = body.cut(bot)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
